import math
import cadquery as cq

# ---------------------------------------------------------------
# Cast bracket: flat base plate with two raised bolt bosses, a bent
# upright ear (three legs in plan, big round-offs at both ends, cross
# hole), a sloping gusset rib from the ear down to the front boss and
# a small round-topped locating tab on the back of the ear.
# Dimensions are given in drawing units and scaled by SCALE to mm.
# X = along the base, Y = across (back edge at +Y), Z = up.
# ---------------------------------------------------------------
SCALE = 0.5

# --- base -------------------------------------------------------
BASE_T = 24.5            # base plate thickness
BACK_Y = 216.1           # straight back edge of the base
C1 = (82.5, 178.8)       # rear bolt boss centre
C2 = (196.8, 39.1)       # front bolt boss centre
R1_BASE = 37.3           # base outline radius round boss 1
R2_BASE = 38.5           # base outline radius round boss 2
P_A = (163.7, 167.4)     # facet corners on the right hand side
P_B = (199.7, 123.4)
BASE_EDGE_R = 4.5        # round on the top outer edge of the base

# --- bosses / holes ---------------------------------------------
BOSS_R = 33.0
BOSS_TOP = 31.0
BOSS_EDGE_R = 4.5
HOLE_D = 32.0

# --- upright ear --------------------------------------------------
EAR_T = 19.5             # wall thickness
EAR_H = 105.0            # height of the flat top
A_X = 65.5               # outer face of the short straight (front) leg
A_Y0 = 79.0              # front end of the ear
A_Y1 = 105.0             # first bend (outer)
ANG_B = 23.0             # middle leg angle from +Y (towards -X)
ANG_C_OUT = 47.0         # rear leg angle, outer face
ANG_C_IN = 45.0          # rear leg angle, inner face
EAR_BACK_Y = 211.0       # rear face of the ear (set in from the base back edge)
BACK_OUT_X = -0.6        # rear leg outer corner / left edge of the base
BACK_IN_X = 25.0         # rear leg inner face, X where it would meet BACK_Y
R_BEND1_OUT, R_BEND1_IN = 6.0, 16.0
R_BEND2_OUT, R_BEND2_IN = 60.0, 90.0
R_BACK_CORNER = 4.8       # base corner at the back left
R_EAR_BACK = 0.0          # ear rear corners (sharp)
R_END_OUT, R_END_IN = 4.0, 8.0

# front end of ear: large round on the top front edge, axis skewed about Z
FR_SKEW = 18.0           # skew of the rounding axis (deg, about Z)
FR_R = 35.0              # rounding radius

# rear end of ear: big round-off in the side profile
ARC_C = (110.0, 15.1)
ARC_R = 110.6
REAR_BLEND_R = 28.0
REAR_SKEW = 6.5          # outer side of the rear round-off sits a bit lower
REAR_SKEW_X = 30.0

EAR_TOP_R = 3.5          # round on the top edges of the ear

EAR_HOLE_D = 21.0
EAR_HOLE_Z = 85.6
EAR_HOLE_S = 40.2        # position along middle leg (from first bend)

# --- tab on back of ear ---------------------------------------------
TAB_W = 21.0             # width along the ear (top is a half round)
TAB_P = 17.0             # projection from the ear
TAB_H = 56.7
TAB_S = 38.6
TAB_EDGE_R = 3.5

# --- gusset rib -----------------------------------------------------
RIB_Y = 114.5
RIB_T = 16.0
RIB_END_X = 192.0
RIB_SLOPE = 0.414
RIB_ARC_C = (135.7, 117.0)
RIB_ARC_R = 56.6
RIB_TOP_Z = 99.0         # where the rib runs into the ear
RIB_NOSE_R = 6.5
RIB_TOP_R = 4.0
RIB_FOOT_R = 4.0


# =================================================================
def unit(v):
    l = math.hypot(v[0], v[1])
    return (v[0] / l, v[1] / l)


def rounded_ops(pts, radii, closed=True):
    """Polyline with per-vertex round radius -> list of path ops."""
    n = len(pts)
    corners = []
    for i in range(n):
        p = pts[i]
        r = radii[i]
        if r <= 0 or (not closed and (i == 0 or i == n - 1)):
            corners.append((p, None, p))
            continue
        a = pts[i - 1]
        b = pts[(i + 1) % n]
        u1 = unit((a[0] - p[0], a[1] - p[1]))
        u2 = unit((b[0] - p[0], b[1] - p[1]))
        cosang = max(-1.0, min(1.0, u1[0] * u2[0] + u1[1] * u2[1]))
        half = math.acos(cosang) / 2.0
        t = r / math.tan(half)
        t1 = (p[0] + t * u1[0], p[1] + t * u1[1])
        t2 = (p[0] + t * u2[0], p[1] + t * u2[1])
        bis = unit((u1[0] + u2[0], u1[1] + u2[1]))
        dm = r / math.sin(half) - r
        m = (p[0] + dm * bis[0], p[1] + dm * bis[1])
        corners.append((t1, m, t2))
    ops = [("M", corners[0][2])]
    rng = range(1, n) if not closed else list(range(1, n)) + [0]
    for i in rng:
        t1, m, t2 = corners[i]
        ops.append(("L", t1))
        if m is not None:
            ops.append(("A", m, t2))
    return ops


def apply_ops(wp, ops, start=True):
    for op in ops:
        if op[0] == "M":
            wp = wp.moveTo(*op[1]) if start else wp.lineTo(*op[1])
        elif op[0] == "L":
            wp = wp.lineTo(*op[1])
        else:
            wp = wp.threePointArc(op[1], op[2])
    return wp


def tangent_point(c, r, p, pick):
    dx, dy = p[0] - c[0], p[1] - c[1]
    d = math.hypot(dx, dy)
    a = math.atan2(dy, dx)
    off = math.acos(r / d)
    cands = [a + off, a - off]
    pts = [(c[0] + r * math.cos(t), c[1] + r * math.sin(t), t) for t in cands]
    return pick(pts)


def pol(c, r, ang):
    return (c[0] + r * math.cos(ang), c[1] + r * math.sin(ang))


def line_isect(p, d, q, e):
    det = d[0] * (-e[1]) - d[1] * (-e[0])
    rx, ry = q[0] - p[0], q[1] - p[1]
    a = (rx * (-e[1]) - ry * (-e[0])) / det
    return (p[0] + a * d[0], p[1] + a * d[1])


def dirv(ang_from_y):
    a = math.radians(ang_from_y)
    return (-math.sin(a), math.cos(a))


# ---------------- upright plan geometry ----------------------------
dB = dirv(ANG_B)
nB = (dB[1], -dB[0])                         # inner-face normal of middle leg
o1 = (A_X, A_Y1)
o3a = (BACK_OUT_X, EAR_BACK_Y)      # ear rear outer corner
o3 = (BACK_OUT_X, BACK_Y)           # base back-left corner
o2 = line_isect(o1, dB, o3a, dirv(ANG_C_OUT))

i_x = A_X + EAR_T
pB_in = (o1[0] + EAR_T * nB[0], o1[1] + EAR_T * nB[1])
i1 = line_isect((i_x, 0.0), (0.0, 1.0), pB_in, dB)
dCi = dirv(ANG_C_IN)
i3 = (BACK_IN_X - (BACK_Y - EAR_BACK_Y) / dCi[1] * dCi[0], EAR_BACK_Y)
i2 = line_isect(pB_in, dB, i3, dCi)

v0 = (A_X, A_Y0)
v7 = (i_x, A_Y0)
ear_pts = [v0, o1, o2, o3a, i3, i2, i1, v7]
ear_rad = [R_END_OUT, R_BEND1_OUT, R_BEND2_OUT, R_EAR_BACK, R_EAR_BACK,
           R_BEND2_IN, R_BEND1_IN, R_END_IN]

# ---------------- base ------------------------------------------
t1 = tangent_point(C1, R1_BASE, P_A, lambda pts: max(pts, key=lambda q: q[1]))
t2 = tangent_point(C2, R2_BASE, P_B, lambda pts: max(pts, key=lambda q: q[0]))
t3 = tangent_point(C2, R2_BASE, v0, lambda pts: min(pts, key=lambda q: q[1]))

m1 = pol(C1, R1_BASE, (math.pi / 2 + t1[2]) / 2)
a2 = t2[2]
a3 = t3[2]
while a3 > a2:
    a3 -= 2 * math.pi
m2 = pol(C2, R2_BASE, (a2 + a3) / 2)

# left side of the base follows the outer face of the ear
left_ops = rounded_ops([(t3[0], t3[1]), v0, o1, o2, o3a, o3, (C1[0], BACK_Y)],
                       [0, 0, R_BEND1_OUT, R_BEND2_OUT, 0, R_BACK_CORNER, 0],
                       closed=False)
wp = cq.Workplane("XY").moveTo(t3[0], t3[1])
wp = apply_ops(wp, left_ops[1:])
wp = (
    wp.threePointArc(m1, (t1[0], t1[1]))
    .lineTo(*P_A)
    .lineTo(*P_B)
    .lineTo(t2[0], t2[1])
    .threePointArc(m2, (t3[0], t3[1]))
    .close()
)
base = wp.extrude(BASE_T)


# round the top outline, except along the left side where the ear sits


def under_ear(e):
    c = e.Center()
    return c.x < A_X + 1.0 and A_Y0 - 1.0 < c.y < EAR_BACK_Y + 1.0


base_top = [e for e in base.faces(">Z").edges().vals() if not under_ear(e)]
base = base.newObject(base_top).fillet(BASE_EDGE_R)

# bosses
for c in (C1, C2):
    boss = (cq.Workplane("XY").center(*c).circle(BOSS_R)
            .extrude(BOSS_TOP - BASE_T + 2).translate((0, 0, BASE_T - 2))
            .faces(">Z").edges().fillet(BOSS_EDGE_R))
    base = base.union(boss)

# ---------------- upright ---------------------------------------
ear_wp = apply_ops(cq.Workplane("XY"), rounded_ops(ear_pts, ear_rad)).close()
ear = ear_wp.extrude(EAR_H).faces(">Z").edges().fillet(EAR_TOP_R)

# rear round-off (side profile, extruded along X): flat top -> blend
# radius -> large arc running down to the back edge
zb = EAR_H - REAR_BLEND_R
yb = ARC_C[0] + math.sqrt((ARC_R - REAR_BLEND_R) ** 2 - (zb - ARC_C[1]) ** 2)
ub = unit((yb - ARC_C[0], zb - ARC_C[1]))
p_bt = (ARC_C[0] + ARC_R * ub[0], ARC_C[1] + ARC_R * ub[1])     # blend -> big arc
ub_m = unit((ub[0], ub[1] + 1.0))
p_bm = (yb + REAR_BLEND_R * ub_m[0], zb + REAR_BLEND_R * ub_m[1])
y_arc1 = BACK_Y + 3.0
z_arc1 = ARC_C[1] + math.sqrt(ARC_R ** 2 - (y_arc1 - ARC_C[0]) ** 2)
am = 0.5 * (math.atan2(p_bt[1] - ARC_C[1], p_bt[0] - ARC_C[0]) +
            math.atan2(z_arc1 - ARC_C[1], y_arc1 - ARC_C[0]))
arc_mid = (ARC_C[0] + ARC_R * math.cos(am), ARC_C[1] + ARC_R * math.sin(am))
rear_cut = (
    cq.Workplane("YZ", origin=(-50, 0, 0))
    .moveTo(yb, EAR_H + 30)
    .lineTo(yb, EAR_H)
    .threePointArc(p_bm, p_bt)
    .threePointArc(arc_mid, (y_arc1, z_arc1))
    .lineTo(y_arc1 + 10, z_arc1)
    .lineTo(y_arc1 + 10, EAR_H + 30)
    .close()
    .extrude(300)
    .rotate((REAR_SKEW_X, EAR_BACK_Y, 0), (REAR_SKEW_X, EAR_BACK_Y, 1), REAR_SKEW)
)
ear = ear.cut(rear_cut)

# front end: large round on the top front edge, on an axis skewed about Z
ps = math.radians(FR_SKEW)
e_ax = cq.Vector(math.cos(ps), math.sin(ps), 0)
f_ax = cq.Vector(-math.sin(ps), math.cos(ps), 0)


def fv(y):
    """Y on the outer face of the front leg -> coordinate in skewed plane"""
    return -A_X * math.sin(ps) + y * math.cos(ps)


v0c = fv(A_Y0)                          # front end face (outer corner)
fr_plane = cq.Plane(origin=(0, 0, 0), xDir=f_ax, normal=e_ax)
qm = (v0c + FR_R - FR_R * math.cos(math.pi / 4),
      EAR_H - FR_R + FR_R * math.sin(math.pi / 4))
front_cut = (
    cq.Workplane(fr_plane)
    .moveTo(v0c - 40.0, EAR_H - FR_R - 40.0)
    .lineTo(v0c, EAR_H - FR_R)
    .threePointArc(qm, (v0c + FR_R, EAR_H))
    .lineTo(v0c + FR_R, EAR_H + 30)
    .lineTo(v0c - 40.0, EAR_H + 30)
    .close()
    .extrude(200, both=True)
)
ear = ear.cut(front_cut)

# ---------------- tab on the back of the ear -------------------------
p_tab = (o1[0] + TAB_S * dB[0], o1[1] + TAB_S * dB[1])     # on the outer face
tab_org = (p_tab[0] + 5.0 * nB[0], p_tab[1] + 5.0 * nB[1], 0.0)
tab_plane = cq.Plane(origin=tab_org, xDir=(-dB[0], -dB[1], 0), normal=(-nB[0], -nB[1], 0))
tab = (
    cq.Workplane(tab_plane)
    .moveTo(-TAB_W / 2, 0)
    .lineTo(TAB_W / 2, 0)
    .lineTo(TAB_W / 2, TAB_H - TAB_W / 2)
    .threePointArc((0, TAB_H), (-TAB_W / 2, TAB_H - TAB_W / 2))
    .close()
    .extrude(TAB_P + 5.0)
)
tab_tip = (p_tab[0] - TAB_P * nB[0], p_tab[1] - TAB_P * nB[1])
tip_edges = [e for e in tab.edges().vals()
             if e.Center().z > 0.5
             and abs((e.Center().x - tab_tip[0]) * nB[0] + (e.Center().y - tab_tip[1]) * nB[1]) < 0.5]
tab = tab.newObject(tip_edges).fillet(TAB_EDGE_R)

# ---------------- gusset rib ----------------------------------------
x_rib_top = RIB_ARC_C[0] - math.sqrt(RIB_ARC_R ** 2 - (RIB_TOP_Z - RIB_ARC_C[1]) ** 2)
nrm = unit((RIB_SLOPE, 1.0))
tp = (RIB_ARC_C[0] - RIB_ARC_R * nrm[0], RIB_ARC_C[1] - RIB_ARC_R * nrm[1])
a_s = math.atan2(RIB_TOP_Z - RIB_ARC_C[1], x_rib_top - RIB_ARC_C[0])
a_e = math.atan2(tp[1] - RIB_ARC_C[1], tp[0] - RIB_ARC_C[0])
if a_e < a_s:
    a_e += 2 * math.pi
rib_mid = (RIB_ARC_C[0] + RIB_ARC_R * math.cos((a_s + a_e) / 2),
           RIB_ARC_C[1] + RIB_ARC_R * math.sin((a_s + a_e) / 2))
z_end = tp[1] - RIB_SLOPE * (RIB_END_X - tp[0])

rib = (
    cq.Workplane("XZ", origin=(0, RIB_Y + RIB_T / 2, 0))
    .moveTo(70, 10)
    .lineTo(70, RIB_TOP_Z)
    .lineTo(x_rib_top, RIB_TOP_Z)
    .threePointArc(rib_mid, tp)
    .lineTo(RIB_END_X, z_end)
    .lineTo(RIB_END_X, 10)
    .close()
    .extrude(RIB_T)
)
rib = rib.edges("|Z").edges(">X").fillet(RIB_NOSE_R)
rib_top_edges = [e for e in rib.edges().vals()
                 if e.Center().z > BASE_T + 1 and e.Center().x > x_rib_top - 1
                 and abs(e.Center().y - RIB_Y) > RIB_T / 2 - 0.5]
rib = rib.newObject(rib_top_edges).fillet(RIB_TOP_R)

part = base.union(ear).union(rib).union(tab)

# blend the rib into the base
rib_foot = [e for e in part.edges().vals()
            if abs(e.Center().z - BASE_T) < 0.6
            and abs(e.Center().y - RIB_Y) < RIB_T / 2 + 0.6
            and e.Center().x > A_X + EAR_T + 1]
part = part.newObject(rib_foot).fillet(RIB_FOOT_R)

# ---------------- holes ---------------------------------------------
for c in (C1, C2):
    part = part.cut(
        cq.Workplane("XY").center(*c).circle(HOLE_D / 2).extrude(100).translate((0, 0, -10))
    )

ho = (o1[0] + EAR_HOLE_S * dB[0], o1[1] + EAR_HOLE_S * dB[1])
hc = (ho[0] + EAR_T / 2 * nB[0], ho[1] + EAR_T / 2 * nB[1])
ear_hole = (
    cq.Workplane("YZ")
    .circle(EAR_HOLE_D / 2)
    .extrude(80)
    .translate((-40, 0, 0))
    .rotate((0, 0, 0), (0, 0, 1), ANG_B)
    .translate((hc[0], hc[1], EAR_HOLE_Z))
)
part = part.cut(ear_hole)

result = cq.Workplane("XY").add(part.val().scale(SCALE))
